import math
import cadquery as cq

# ---------------------------------------------------------------
# Thin-walled bell / horn shell: trumpet-flared lip at -X, narrow
# neck, half-ellipsoid bowl opening at +X.  Axis of revolution = X.
#
# outer profile (x along axis, r radial):
#   lip  : quarter-ellipse, vertical tangent at the rim (x=0, r=RIM_R),
#          lowest point r=NECK_R, then rising until it becomes
#          tangent to ...
#   bowl : half-ellipse whose equator is the open end (x=BODY_LEN,
#          r=BODY_R) and whose apex lies just behind the rim plane
# inner profile = same construction offset by WALL.
# ---------------------------------------------------------------

# driving dimensions (mm)
BODY_LEN = 138.0      # rim plane -> open end (bowl semi-axis along X)
BODY_R = 50.0         # outer radius of the open end (bowl radial semi-axis)
RIM_R = 43.7          # outer radius of the flared lip
NECK_R = 23.9         # smallest outer radius of the neck
BOWL_APEX = 1.0       # bowl ellipse apex sits this far behind the rim plane
WALL = 0.25           # shell wall thickness

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- profile helpers (pure math) -------------------
def r_bowl(x, A, Bb):
    """bowl ellipse, centre (BODY_LEN, 0), semi-axes (A, Bb)"""
    c = (x - BODY_LEN) / A
    return Bb * math.sqrt(max(0.0, 1.0 - c * c))


def r_lip(x, xc, a, b):
    """lower branch of lip ellipse, centre (xc, RIM_R), semi-axes (a, b)"""
    c = (x - xc) / a
    return RIM_R - b * math.sqrt(max(0.0, 1.0 - c * c))


def min_gap(xc, a, b, A, Bb):
    """min over x of r_lip - r_bowl on the rising side of the lip"""
    lo, hi = xc, xc + 0.999 * a
    f = lambda x: r_lip(x, xc, a, b) - r_bowl(x, A, Bb)
    for _ in range(200):  # ternary search (unimodal there)
        m1 = lo + (hi - lo) / 3.0
        m2 = hi - (hi - lo) / 3.0
        if f(m1) < f(m2):
            hi = m2
        else:
            lo = m1
    xm = 0.5 * (lo + hi)
    return f(xm), xm


def bisect(fun, lo, hi, n=200):
    """root of a monotone function (sign(fun(lo)) != sign(fun(hi)))"""
    flo = fun(lo)
    for _ in range(n):
        mid = 0.5 * (lo + hi)
        fm = fun(mid)
        if (fm > 0) == (flo > 0):
            lo, flo = mid, fm
        else:
            hi = mid
    return 0.5 * (lo + hi)


# outer lip: rim at x=0 -> centre x = a ; depth b = RIM_R - NECK_R ;
# choose a so that the lip just touches (is tangent to) the bowl.
A_o, B_o = BODY_LEN + BOWL_APEX, BODY_R
b_o = RIM_R - NECK_R
a_o = bisect(lambda a: min_gap(a, a, b_o, A_o, B_o)[0], 6.0, 30.0)
XC = a_o                                   # lip ellipse centre (x)
xt_o = min_gap(XC, a_o, b_o, A_o, B_o)[1]   # outer tangent point

# inner lip / bowl, offset by the wall
A_i, B_i = A_o - WALL, B_o - WALL
a_i = a_o + WALL
b_i = bisect(lambda b: min_gap(XC, a_i, b, A_i, B_i)[0], b_o - 3.0, b_o + 3.0)
xt_i = min_gap(XC, a_i, b_i, A_i, B_i)[1]


# ---------------- edges -----------------------------------------
def P(x, r):
    # profile drawn in the XZ plane (radius along +Z)
    return cq.Vector(x, 0.0, r)


N = cq.Vector(0, -1, 0)   # ellipse plane normal so that local Y = +Z
XD = cq.Vector(1, 0, 0)


def lip_arc(a, b, x_end):
    c = (x_end - XC) / a
    th = 360.0 - math.degrees(math.acos(max(-1.0, min(1.0, c))))
    return cq.Edge.makeEllipse(a, b, P(XC, RIM_R), N, XD, 180.0, th, 1)


def bowl_arc(A, Bb, x_start):
    c = (x_start - BODY_LEN) / A
    ph = math.degrees(math.acos(max(-1.0, min(1.0, c))))
    return cq.Edge.makeEllipse(A, Bb, P(BODY_LEN, 0.0), N, XD, 90.0, ph, 1)


e1 = lip_arc(a_o, b_o, xt_o)                       # rim -> neck (outer)
e2 = bowl_arc(A_o, B_o, xt_o)                      # neck -> open end (outer)
e3 = cq.Edge.makeLine(P(BODY_LEN, BODY_R), P(BODY_LEN, BODY_R - WALL))
e4 = bowl_arc(A_i, B_i, xt_i)                      # open end -> neck (inner)
e5 = lip_arc(a_i, b_i, xt_i)                       # neck -> rim (inner)
e6 = cq.Edge.makeLine(P(XC - a_i, RIM_R), P(0.0, RIM_R))   # rim lip face

# the neck junction splits the wall into the flared lip and the bowl
ej = cq.Edge.makeLine(e1.endPoint(), e4.endPoint())
lip_profile = cq.Wire.assembleEdges([e1, ej, e5, e6])
bowl_profile = cq.Wire.assembleEdges([e2, e3, e4, ej])

AX0, AX1 = cq.Vector(0, 0, 0), cq.Vector(1, 0, 0)
lip = cq.Solid.revolve(lip_profile, [], 360.0, AX0, AX1)
lip = lip.rotate(AX0, AX1, -90.0)          # lip seam on the +Y side, bowl seam on top
bowl = cq.Solid.revolve(bowl_profile, [], 360.0, AX0, AX1)

shell = bowl.fuse(lip).clean()
result = cq.Workplane("XY").add(shell)
